import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
R_BODY = 50.3        # outer radius of main body
H = 162.6            # overall height
R_RIM = 54.8         # outer radius of top rim flange
H_RIM = 8.4          # height of vertical outer rim band
# rim -> body transition: two conical facets (shallow upper, steeper lower)
DZ1 = 1.6            # height of upper (shallow) facet
A1 = 37.0            # upper facet angle below horizontal (deg)
DZ2 = 2.4            # height of lower (steeper, ~45 deg) facet
C_BOT = 3.6          # 45 deg chamfer on the bottom outer edge
T_TOP = 1.1          # width of the rim top face (wall thickness at the lip)
R_IN = 48.75         # inner bore radius of the body
D_FLARE = 14.3       # depth of the inner conical flare below the top
T_FLOOR = 4.0        # floor thickness
F_FLOOR = 1.5        # inner floor fillet radius
BUMP_D = 3.3         # locating bump (spherical cap) base diameter
BUMP_H = 1.1         # bump protrusion
BUMP_DROP = 21.4     # bump centre distance below top
SEAM_ANGLE = 45.0    # angular position of the revolve seam (cosmetic)

# ---------------- revolved body profile (r, z) ----------------
z_rim_bot = H - H_RIM
r_mid = R_RIM - DZ1 / math.tan(math.radians(A1))
z_mid = z_rim_bot - DZ1
z_body_top = z_mid - DZ2

outer = [
    (0.0, 0.0),
    (R_BODY - C_BOT, 0.0),
    (R_BODY, C_BOT),
    (R_BODY, z_body_top),
    (r_mid, z_mid),
    (R_RIM, z_rim_bot),
    (R_RIM, H),
    (R_RIM - T_TOP, H),          # inner lip edge
    (R_IN, H - D_FLARE),         # bottom of inner flare
    (R_IN, T_FLOOR + F_FLOOR),
]

# inner floor fillet as an arc in the profile
fc = (R_IN - F_FLOOR, T_FLOOR + F_FLOOR)
fm = (fc[0] + F_FLOOR * math.cos(math.radians(-45)), fc[1] + F_FLOOR * math.sin(math.radians(-45)))
prof = (
    cq.Workplane("XZ")
    .polyline(outer)
    .threePointArc(fm, (R_IN - F_FLOOR, T_FLOOR))
    .lineTo(0.0, T_FLOOR)
    .close()
)
body = prof.revolve(360.0, (0, 0, 0), (0, 1, 0))
# turn the revolve seam to the 45 deg diagonal
body = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)

# ---------------- two small bumps on the outside, at +Y and -Y ----------------
a = BUMP_D / 2.0
rs = (a ** 2 + BUMP_H ** 2) / (2 * BUMP_H)       # sphere radius of the cap
zc = H - BUMP_DROP
core = cq.Workplane("XY").circle(R_BODY - 0.01).extrude(H)
for sgn in (1, -1):
    c = R_BODY + BUMP_H - rs
    sph = cq.Workplane("XY").sphere(rs).translate((0, sgn * c, zc))
    body = body.union(sph.cut(core))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
